import math
import cadquery as cq

# ---------------------------------------------------------------------------
# Multi-body moulded kit: a hooked back rail with six tabs, a main cover plate
# (flat back part, curved inclined front part, oval and rectangular recesses),
# two mirrored wedge-shaped levers (C bracket, post, bridge, rib), two small
# pin hinges and two curved strips with end pads.
# Layout is measured in a "drawing" frame: X 0..237 (length), Y 0..194
# (front -> back), Z 0..39.  Everything is shifted to be centred at the end.
# ---------------------------------------------------------------------------
L = 237.0            # overall length (rail / main plate)
XC = 118.6           # symmetry X of the layout

# ---- rail (back, J profile) ----
RAIL_Y0, RAIL_Y1 = 178.0, 193.6
RAIL_Z0 = 3.8        # bottom of the rounded body
RAIL_LEDGE = 10.2    # top of the back ledge
RAIL_ARM_T = 3.5     # thickness of the front arm
RAIL_ARM_TOP = 15.7  # top of the front arm
TAB_W = 10.0
TAB_Y0 = 188.2
TAB_TOP = 20.4
TAB_CX = [10.0, 35.0, 102.0, 134.0, 200.5, 225.6]

# ---- main plate ----
MP_Y_BACK = 173.9
MP_Y_STEP = 124.0
MP_FRONT_X0, MP_FRONT_X1 = 25.7, 211.6
MP_TOP = 13.2                    # top of the flat back part
MP_BOT = 9.6                     # underside of the flat back part
# inclined front part: (y, z_top, z_bottom) at front tip, step and crease
INC = [(105.5, 10.9, 6.4), (123.0, 12.3, 7.9), (139.5, 15.3, 10.9)]
BLOCK_Y0, BLOCK_Y1, BLOCK_Z0 = 147.2, 158.2, 3.8
FOOT_L = 10.0                    # feet under both ends of the plate
LIP_Y0, LIP_Z0 = 169.8, 5.1
LIP_FILLET = 1.5
OVAL = (17.7, 48.5, 146.8, 165.5)        # x0,x1,y0,y1
POCKET = (124.7, 203.9, 111.0, 133.4)    # x0,x1,y0,y1
RECESS = 0.9
MP_EDGE_R = 1.2

# ---- wedge plates ----
W_Z0, W_Z1 = 6.3, 14.6
W1_PTS = [(5.7, 100.3), (6.6, 61.8), (185.7, 85.4), (185.7, 100.3)]
W_CORNER_R = 19.0                         # big round at the wide end
W_TIP_R_BACK, W_TIP_R_FRONT = 6.0, 3.0    # rounds at the narrow end
W_EDGE_R = 1.2                            # top / bottom edge rounds
W2_DX, W2_DY = 238.3, -54.0              # wedge 2 = mirror(X) + shift
W1_DZ = -1.3                              # wedge 1 sits a little lower
CB = dict(cx=174.8, cy=89.9, w=8.7, d=11.4, top=38.8, ang=9.0,
          nz0=20.5, nz1=30.4, ndepth=5.6)  # C bracket
POST = dict(x0=30.1, x1=43.4, y0=76.2, y1=82.9, top=26.6, ang=6.0)
BRIDGE = dict(x0=14.4, x1=41.1, y0=92.4, y1=96.4, top=27.3, leg=4.4, bar=5.0)
RIB = dict(xa=103.0, xb=161.5, w=3.4, h=4.8, inset=3.6)

# ---- hinges ----
H1 = (214.6, 90.5)
H2 = (35.1, 45.5)
H_LEAF = [(-20.3, 5.2), (-9.0, 5.2), (-1.0, 2.4), (-1.0, -0.6),
          (-6.0, -1.4), (-9.0, -2.6), (-20.3, 1.3)]
H_KNUCKLES = [(24.7, 28.2), (13.1, 22.9), (8.1, 11.7)]
H_LUG_X0 = -7.0
H_R_BARREL, H_R_PIN = 3.2, 2.0
H_PIN_Z = (4.0, 31.6)
H_Z = (8.1, 28.2)

# ---- curved strips ----
S2_P = [(13.4, 25.0), (70.0, 14.5), (125.0, 10.6)]
S_W = 9.8            # band + groove + fin
S_FIN_W = 3.0
S_GAP = 0.6
S_GROOVE_D = 3.0
S_BAND_R = 2.2          # chamfer on the front top edge of the band
S_FIN_EXT = 2.4
S_H = 5.2
S_TAB_H = 5.2
S_TAB_L = (3.6, 14.6, 10.8, 29.4)        # end pads (x0, x1, y0, y1)
S_TAB_R = (113.8, 125.4, -0.2, 12.2)
S1_DX, S1_MIRROR_Y, S1_DZ = 106.5, 41.5, 4.0


def box(x0, x1, y0, y1, z0, z1):
    return (cq.Workplane("XY")
            .box(x1 - x0, y1 - y0, z1 - z0, centered=False)
            .translate((x0, y0, z0)))


# ---------------------------------------------------------------- rail
def make_rail():
    body = box(0, L, RAIL_Y0, RAIL_Y1, RAIL_Z0, RAIL_LEDGE)
    body = body.edges("|X and <Z").edges(">Y").fillet(5.8)
    body = body.edges("|X and <Z").edges("<Y").fillet(3.5)
    arm = box(0, L, RAIL_Y0, RAIL_Y0 + RAIL_ARM_T, RAIL_Z0 + 4, RAIL_ARM_TOP)
    arm = arm.edges("|X and >Z").fillet(1.2)
    rail = body.union(arm)
    for cx in TAB_CX:
        t = box(cx - TAB_W / 2, cx + TAB_W / 2, TAB_Y0, RAIL_Y1,
                RAIL_LEDGE - 1.0, TAB_TOP)
        t = t.edges("|Y and >Z").fillet(1.5)
        rail = rail.union(t)
    return rail


# ---------------------------------------------------------------- main plate
def make_main_plate():
    (ya, ta, ba), (yb, tb, bb), (yc, tc, bc) = INC
    # profile: gently curved (concave) inclined front part with rounded
    # front edges, crease ridge, flat back part
    r = MP_EDGE_R
    k = math.sin(math.pi / 4)
    wp = (cq.Workplane("YZ").moveTo(ya, ba + r)
          .threePointArc((ya + r - r * k, ba + r - r * k), (ya + r, ba))
          .threePointArc((yb, bb), (yc - 3.0, bc - 0.4))
          .lineTo(yc + 1.5, MP_BOT)
          .lineTo(MP_Y_BACK, MP_BOT).lineTo(MP_Y_BACK, MP_TOP)
          .lineTo(yc + 1.0, MP_TOP).lineTo(yc, tc)
          .threePointArc((yb, tb), (ya + r, ta))
          .threePointArc((ya + r - r * k, ta - r + r * k), (ya, ta - r))
          .close())
    full = wp.extrude(L)
    # plan outline: the front strip (ahead of the step) is narrower
    plan = (cq.Workplane("XY", origin=(0, 0, -10))
            .polyline([(MP_FRONT_X0, ya), (MP_FRONT_X1, ya),
                       (MP_FRONT_X1, MP_Y_STEP), (L, MP_Y_STEP),
                       (L, MP_Y_BACK), (0, MP_Y_BACK), (0, MP_Y_STEP),
                       (MP_FRONT_X0, MP_Y_STEP)]).close()
            .extrude(50))
    plan = plan.edges("|Z").edges(cq.selectors.BoxSelector(
        (-5, ya - 1, -20), (L + 5, ya + 1, 50))).fillet(3.0)
    plan = plan.edges("|Z").edges(cq.selectors.BoxSelector(
        (-5, MP_Y_STEP - 1, -20), (L + 5, MP_Y_BACK + 1, 50))).fillet(1.0)
    plate = full.intersect(plan)
    # feet under both ends and the back lip (rounded inner corner)
    for fx0 in (0.0, L - FOOT_L):
        plate = plate.union(box(fx0, fx0 + FOOT_L, BLOCK_Y0, BLOCK_Y1,
                                BLOCK_Z0, MP_BOT + 0.5))
    rl = LIP_FILLET
    c45 = rl * (1 - math.cos(math.pi / 4))
    lip = (cq.Workplane("YZ").moveTo(LIP_Y0, LIP_Z0)
           .lineTo(MP_Y_BACK, LIP_Z0).lineTo(MP_Y_BACK, MP_BOT + 0.5)
           .lineTo(LIP_Y0 - rl, MP_BOT + 0.5).lineTo(LIP_Y0 - rl, MP_BOT)
           .threePointArc((LIP_Y0 - c45, MP_BOT - c45), (LIP_Y0, MP_BOT - rl))
           .close().extrude(L))
    plate = plate.union(lip)
    # oval recess in the back part
    ox0, ox1, oy0, oy1 = OVAL
    oval = (cq.Workplane("XY", origin=((ox0 + ox1) / 2, (oy0 + oy1) / 2,
                                       MP_TOP - RECESS))
            .slot2D(ox1 - ox0, oy1 - oy0).extrude(5))
    plate = plate.cut(oval)
    # rectangular recess in the inclined front part
    px0, px1, py0, py1 = POCKET
    slab = (cq.Workplane("YZ", origin=(px0, 0, 0))
            .moveTo(yc, tc - RECESS)
            .threePointArc((yb, tb - RECESS), (ya + MP_EDGE_R, ta - RECESS))
            .lineTo(ya + MP_EDGE_R, ta + 5).lineTo(yc, tc + 5).close()
            .extrude(px1 - px0))
    rr = (cq.Workplane("XY", origin=((px0 + px1) / 2, (py0 + py1) / 2, 0))
          .rect(px1 - px0, py1 - py0).extrude(30)
          .edges("|Z").fillet(2.5))
    plate = plate.cut(slab.intersect(rr))
    return plate


# ---------------------------------------------------------------- wedges
def make_wedge():
    base = (cq.Workplane("XY", origin=(0, 0, W_Z0))
            .polyline(W1_PTS).close().extrude(W_Z1 - W_Z0))
    base = base.edges("|Z").edges(cq.selectors.NearestToPointSelector(
        (W1_PTS[1][0], W1_PTS[1][1], 10))).fillet(W_CORNER_R)
    base = base.edges("|Z").edges(cq.selectors.NearestToPointSelector(
        (W1_PTS[3][0], W1_PTS[3][1], 10))).fillet(W_TIP_R_BACK)
    base = base.edges("|Z").edges(cq.selectors.NearestToPointSelector(
        (W1_PTS[2][0], W1_PTS[2][1], 10))).fillet(W_TIP_R_FRONT)
    base = base.faces(">Z").edges().fillet(W_EDGE_R)
    base = base.faces("<Z").edges().fillet(W_EDGE_R)
    # C bracket at the narrow end (notch open to -Y)
    c = CB
    hw, hd = c["w"] / 2, c["d"] / 2
    cb = box(-hw, hw, -hd, hd, W_Z1 - 0.5, c["top"])
    cb = cb.edges(">Z").fillet(0.8)
    cb = cb.cut(box(-hw - 1, hw + 1, -hd - 1, -hd + c["ndepth"],
                    c["nz0"], c["nz1"]))
    cb = (cb.rotate((0, 0, 0), (0, 0, 1), c["ang"])
          .translate((c["cx"], c["cy"], 0)))
    w = base.union(cb)
    # square post at the wide end
    p = POST
    pcx, pcy = (p["x0"] + p["x1"]) / 2, (p["y0"] + p["y1"]) / 2
    post = box(p["x0"], p["x1"], p["y0"], p["y1"], W_Z1 - 0.5, p["top"])
    post = post.edges("|Z").fillet(1.0).faces(">Z").edges().fillet(0.8)
    post = post.rotate((pcx, pcy, 0), (pcx, pcy, 1), p["ang"])
    w = w.union(post)
    # bridge (inverted U) along the back edge at the wide end
    b = BRIDGE
    br = (cq.Workplane("XY", origin=((b["x0"] + b["x1"]) / 2,
                                     (b["y0"] + b["y1"]) / 2, W_Z1 - 0.5))
          .slot2D(b["x1"] - b["x0"], b["y1"] - b["y0"])
          .extrude(b["top"] - W_Z1 + 0.5))
    br = br.faces(">Z").edges().fillet(0.8)
    br = br.cut(box(b["x0"] + b["leg"], b["x1"] - b["leg"], b["y0"] - 1,
                    b["y1"] + 1, W_Z1 - 1, b["top"] - b["bar"]))
    w = w.union(br)
    # rib following the sloped front edge
    (xa, ya), (xb, yb) = W1_PTS[1], W1_PTS[2]
    slope = (yb - ya) / (xb - xa)
    ang = math.degrees(math.atan(slope))
    rx0, rx1 = RIB["xa"], RIB["xb"]
    rmx = (rx0 + rx1) / 2
    rmy = ya + slope * (rmx - xa) + RIB["inset"]
    rib = (cq.Workplane("XY", origin=(0, 0, W_Z1 - 0.5))
           .center(rmx, rmy)
           .transformed(rotate=(0, 0, ang))
           .rect((rx1 - rx0) / math.cos(math.radians(ang)), RIB["w"])
           .extrude(RIB["h"] + 0.5))
    w = w.union(rib)
    return w


def make_wedge1(w):
    return w.translate((0, 0, W1_DZ))


def make_wedge2(w):
    return (w.mirror("YZ", basePointVector=(0, 0, 0))
            .translate((W2_DX, W2_DY, 0)))


# ---------------------------------------------------------------- hinges
def make_hinge(cx, cy):
    z0, z1 = H_Z
    # leaf outline in plan, relative to the pin axis: straight back edge,
    # bevelled front face
    leaf = (cq.Workplane("XY", origin=(0, 0, z0))
            .polyline(H_LEAF).close().extrude(z1 - z0))
    leaf = leaf.edges("|Z").fillet(0.5)
    h = leaf
    # three knuckles: rounded lugs running from the leaf to the pin axis
    r = H_R_BARREL
    for k0, k1 in H_KNUCKLES:
        lug = (cq.Workplane("XY", origin=(0, 0, k0))
               .moveTo(H_LUG_X0, -r).lineTo(0, -r)
               .threePointArc((r, 0), (0, r)).lineTo(H_LUG_X0, r).close()
               .extrude(k1 - k0))
        lug = lug.faces(">Z or <Z").edges().fillet(0.5)
        h = h.union(lug)
    pin = (cq.Workplane("XY", origin=(0, 0, H_PIN_Z[0]))
           .circle(H_R_PIN).extrude(H_PIN_Z[1] - H_PIN_Z[0]))
    h = h.union(pin)
    return h.translate((cx, cy, 0))


# ---------------------------------------------------------------- strips
def _circle3(p1, p2, p3):
    (x1, y1), (x2, y2), (x3, y3) = p1, p2, p3
    d = 2 * (x1 * (y2 - y3) + x2 * (y3 - y1) + x3 * (y1 - y2))
    ux = ((x1 ** 2 + y1 ** 2) * (y2 - y3) + (x2 ** 2 + y2 ** 2) * (y3 - y1)
          + (x3 ** 2 + y3 ** 2) * (y1 - y2)) / d
    uy = ((x1 ** 2 + y1 ** 2) * (x3 - x2) + (x2 ** 2 + y2 ** 2) * (x1 - x3)
          + (x3 ** 2 + y3 ** 2) * (x2 - x1)) / d
    return ux, uy, math.hypot(x1 - ux, y1 - uy)


def _revolved_band(profile, ux, uy, th0, th1):
    """Revolve a closed (rho, z) profile about the vertical axis through
    (ux, uy) between the polar angles th0 < th1 (radians)."""
    wp = cq.Workplane("XZ").moveTo(*profile[0][1])
    for seg in profile[1:]:
        if seg[0] == "L":
            wp = wp.lineTo(*seg[1])
        else:
            wp = wp.threePointArc(seg[1], seg[2])
    solid = wp.close().revolve(math.degrees(th1 - th0), (0, 0, 0), (0, 1, 0))
    return (solid.rotate((0, 0, 0), (0, 0, 1), math.degrees(th0))
            .translate((ux, uy, 0)))


def make_strip2():
    # curved band: wide rounded band at the front, thin fin behind it,
    # separated by a groove.  The centre line is an arc through S2_P.
    ux, uy, r = _circle3(*S2_P)
    (ax, ay), _, (bx, by) = S2_P
    th_a = math.atan2(ay - uy, ax - ux)
    th_b = math.atan2(by - uy, bx - ux)
    th0, th1 = min(th_a, th_b), max(th_a, th_b)
    # radial offset +d points away from the arc centre (= towards the front)
    ro, ri = r + S_W / 2, r - S_W / 2
    rf = ri + S_FIN_W
    rb = rf + S_GAP
    R = S_BAND_R
    prof = [("M", (ri, 0.0)), ("L", (ro, 0.0)), ("L", (ro, S_H - R)),
            ("L", (ro - R, S_H)),
            ("L", (rb, S_H)), ("L", (rb, S_H - S_GROOVE_D)),
            ("L", (rf, S_H - S_GROOVE_D)), ("L", (rf, S_H)),
            ("L", (ri, S_H))]
    s = _revolved_band(prof, ux, uy, th0, th1)
    # the fin runs a little past the right-hand end of the band
    fin_prof = [("M", (ri, 0.0)), ("L", (rf, 0.0)), ("L", (rf, S_H)),
                ("L", (ri, S_H))]
    s = s.union(_revolved_band(fin_prof, ux, uy, th1 - 0.002,
                               th1 + S_FIN_EXT / r))
    lt = box(*S_TAB_L, 0, S_TAB_H)
    rt = box(*S_TAB_R, 0, S_TAB_H)
    lt = lt.edges("|Z").fillet(1.0).faces(">Z").edges().fillet(0.6)
    rt = rt.edges("|Z").fillet(1.0).faces(">Z").edges().fillet(0.6)
    s = s.union(lt).union(rt)
    return s


def make_strip1(s2):
    return (s2.mirror("XZ", basePointVector=(0, S1_MIRROR_Y, 0))
            .translate((S1_DX, 0, S1_DZ)))


# ---------------------------------------------------------------- assemble
rail = make_rail()
plate = make_main_plate()
w0 = make_wedge()
w1 = make_wedge1(w0)
w2 = make_wedge2(w0)
h1 = make_hinge(*H1)
h2 = make_hinge(*H2)
s2 = make_strip2()
s1 = make_strip1(s2)

parts = [rail, plate, w1, w2, h1, h2, s1, s2]
shift = (-XC, -97.0, 0.0)
solids = []
for p in parts:
    for s in p.translate(shift).solids().vals():
        solids.append(s)

result = cq.Workplane("XY").newObject([cq.Compound.makeCompound(solids)])

VIEW = {"azimuth": 45, "elevation": 26}
